import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 150.0          # overall length (X)
T = 1.1            # sheet thickness

W_R = 25.5         # right plate width (Y)
W_L = 19.5         # left plate width
W_S = 13.4         # middle strip width
Y_TOP = W_R / 2.0  # common +Y edge

# Z levels (bottom faces), pins end at z = 0
Z_L = 6.6          # left (high) plate bottom
Z_S = 1.5          # middle strip bottom
Z_R = 3.95         # right plate bottom

# S-bend between left plate and strip
X_B1 = 54.6        # start of first bend
R_B1 = 2.4         # centre-line bend radius
TH_B1 = math.radians(78)

# joggle between strip and right plate
X_B2 = 101.9       # start of joggle
R_B2 = 1.3
TH_B2 = math.radians(80)

X_RP = 106.2       # start of the wide part of the right plate
X_LN = 55.0        # end of the wide part of the left plate
NECK_CR = 2.0      # convex corner where the left plate narrows
NECK_FIL_X = 1.7   # concave (elliptic) fillet into the strip, along X
NECK_FIL_Y = 3.0   # ... and along Y
JOG_FIL = 3.3      # concave fillet strip -> right plate

CORNER_R = 1.6     # outline corner radius (right plate inner corner)
END_R_L = 2.0      # corners at the left end
END_R_R = 1.0      # corners at the right end
NOTCH_W = 7.2      # notch in the right end
NOTCH_D = 1.0

# raised square pad on left plate
PAD_CX = 43.1
PAD_S = 15.2
PAD_H = 0.8
PAD_R = 2.1
PAD_FIL = 0.75
POCKET_X = 10.8
POCKET_Y = 12.4
POCKET_CX = 43.6
POCKET_D = 0.5

# pins (stand-offs)
PIN_D = 2.75
PIN_EDGE_L = 3.05
PIN_EDGE_R = 2.75
PINS_LEFT_X = (2.1, 37.2)
PINS_RIGHT_X = (109.3, 139.0)
PIN_CH = 0.15



# ---------------- side profile of the bent sheet ----------------
def centerline():
    segs = []
    zl = Z_L + T / 2.0
    zs = Z_S + T / 2.0
    zr = Z_R + T / 2.0
    drop = zl - zs
    s1 = (drop - 2 * R_B1 * (1 - math.cos(TH_B1))) / math.sin(TH_B1)
    rise = zr - zs
    s2 = (rise - 2 * R_B2 * (1 - math.cos(TH_B2))) / math.sin(TH_B2)
    segs.append(("L", X_B1))
    segs.append(("A", R_B1, -TH_B1))
    segs.append(("S", s1))
    segs.append(("A", R_B1, TH_B1))
    segs.append(("X", X_B2))
    segs.append(("A", R_B2, TH_B2))
    segs.append(("S", s2))
    segs.append(("A", R_B2, -TH_B2))
    segs.append(("X", L))
    return (0.0, zl), segs


def offset_path(d):
    """Return list of edges of the centre-line offset by d (left = +Z)."""
    (x, z), segs = centerline()
    h = 0.0
    edges = []

    def nl(hh):
        return (-math.sin(hh), math.cos(hh))

    def P(px, pz, hh):
        n = nl(hh)
        return cq.Vector(px + d * n[0], 0, pz + d * n[1])

    for seg in segs:
        if seg[0] in ("L", "X", "S"):
            if seg[0] == "S":
                ln = seg[1]
                nx, nz = x + ln * math.cos(h), z + ln * math.sin(h)
            else:
                nx, nz = seg[1], z + (seg[1] - x) * math.tan(h)
            edges.append(cq.Edge.makeLine(P(x, z, h), P(nx, nz, h)))
            x, z = nx, nz
        else:
            R, a = seg[1], seg[2]
            sgn = 1.0 if a > 0 else -1.0
            n = nl(h)
            cx, cz = x + sgn * R * n[0], z + sgn * R * n[1]

            def pt(ang):
                hh = h + ang
                nn = nl(hh)
                return cx - sgn * R * nn[0], cz - sgn * R * nn[1], hh

            mx, mz, mh = pt(a / 2)
            ex, ez, eh = pt(a)
            edges.append(cq.Edge.makeThreePointArc(P(x, z, h), P(mx, mz, mh), P(ex, ez, eh)))
            x, z, h = ex, ez, eh
    return edges


top = offset_path(T / 2.0)
bot = offset_path(-T / 2.0)
cap_end = cq.Edge.makeLine(top[-1].endPoint(), bot[-1].endPoint())
cap_start = cq.Edge.makeLine(bot[0].startPoint(), top[0].startPoint())
bot_rev = [cq.Edge.makeLine(e.endPoint(), e.startPoint()) if e.geomType() == "LINE"
           else cq.Edge.makeThreePointArc(e.endPoint(), e.positionAt(0.5), e.startPoint())
           for e in reversed(bot)]
wire = cq.Wire.assembleEdges(top + [cap_end] + bot_rev + [cap_start])
face = cq.Face.makeFromWires(wire)
y0 = Y_TOP - W_R - 2.0
sheet_body = cq.Solid.extrudeLinear(face, cq.Vector(0, W_R + 4.0, 0))
sheet_body = sheet_body.translate(cq.Vector(0, y0, 0))
sheet = cq.Workplane("XY").add(sheet_body)

# ---------------- top-view outline ----------------
yb_L = Y_TOP - W_L
yb_S = Y_TOP - W_S
yb_R = Y_TOP - W_R


def rounded_outline(pts, radii):
    """closed axis-aligned polygon with rounded corners.
    radius entry: float (circular) or (r_along_in_edge, r_along_out_edge)
    for an elliptical corner; convex and concave corners both handled."""
    n = len(pts)
    V = [cq.Vector(p[0], p[1], 0) for p in pts]
    Zv = cq.Vector(0, 0, 1)
    corners = []
    arcs = []
    for i in range(n):
        v = V[i]
        r = radii[i]
        d_in = (v - V[i - 1]).normalized()
        d_out = (V[(i + 1) % n] - v).normalized()
        if isinstance(r, tuple):
            r_in, r_out = r
        else:
            r_in = r_out = r
        if r_in <= 0:
            corners.append((v, v))
            arcs.append(None)
            continue
        p_in = v - d_in * r_in
        p_out = v + d_out * r_out
        c = v - d_in * r_in + d_out * r_out
        if abs(r_in - r_out) < 1e-9:
            m = c + (v - c).normalized() * r_in
            arcs.append(cq.Edge.makeThreePointArc(p_in, m, p_out))
        else:
            ux = d_in
            uy = Zv.cross(ux)
            th_in = 90.0 if (-d_out).dot(uy) > 0 else -90.0
            a1, a2 = (0.0, th_in) if th_in > 0 else (th_in, 0.0)
            arcs.append(cq.Edge.makeEllipse(r_in, r_out, c, Zv, ux, a1, a2))
        corners.append((p_in, p_out))
    edges = []
    for i in range(n):
        a = corners[i][1]
        b = corners[(i + 1) % n][0]
        if (b - a).Length > 1e-9:
            edges.append(cq.Edge.makeLine(a, b))
        if arcs[(i + 1) % n] is not None:
            edges.append(arcs[(i + 1) % n])
    w = cq.Wire.assembleEdges(edges)
    return cq.Face.makeFromWires(w)


pts = [
    (0, Y_TOP), (L, Y_TOP),
    (L, NOTCH_W / 2), (L - NOTCH_D, NOTCH_W / 2),
    (L - NOTCH_D, -NOTCH_W / 2), (L, -NOTCH_W / 2),
    (L, yb_R), (X_RP, yb_R), (X_RP, yb_S),
    (X_LN, yb_S), (X_LN, yb_L), (0, yb_L),
]
rad = [END_R_L, END_R_R, 0.25, 0.25, 0.25, 0.25,
       END_R_R, CORNER_R, JOG_FIL, (NECK_FIL_X, NECK_FIL_Y), NECK_CR, END_R_L]
outline = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(rounded_outline(pts, rad), cq.Vector(0, 0, 20)).translate(cq.Vector(0, 0, -2)))

part = sheet.intersect(outline)

# ---------------- raised pad + underside pocket ----------------
yc_L = Y_TOP - W_L / 2.0
pad = (cq.Workplane("XY").workplane(offset=Z_L + T)
       .center(PAD_CX, yc_L).rect(PAD_S, PAD_S).extrude(PAD_H)
       .edges("|Z").fillet(PAD_R).faces(">Z").edges().fillet(PAD_FIL))
part = part.union(pad)
pocket = (cq.Workplane("XY").workplane(offset=Z_L - 1.0)
          .center(POCKET_CX, yc_L).rect(POCKET_X, POCKET_Y).extrude(1.0 + POCKET_D)
          .edges("|Z").fillet(0.8))
part = part.cut(pocket)

# ---------------- pins ----------------
pin_y = (yb_L + PIN_EDGE_L, Y_TOP - PIN_EDGE_L)
pin_yr = (yb_R + PIN_EDGE_R, Y_TOP - PIN_EDGE_R)
for px in PINS_LEFT_X:
    for py in pin_y:
        pin = (cq.Workplane("XY").center(px, py).circle(PIN_D / 2).extrude(Z_L + 0.2)
               .faces("<Z").edges().chamfer(PIN_CH))
        part = part.union(pin)
for px in PINS_RIGHT_X:
    for py in pin_yr:
        pin = (cq.Workplane("XY").center(px, py).circle(PIN_D / 2).extrude(Z_R + 0.2)
               .faces("<Z").edges().chamfer(PIN_CH))
        part = part.union(pin)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
